"""Ribbed barrel cactus on a round base plate.

The fluted body has a 12-point star cross-section whose size follows a barrel + dome
profile.  It is built exactly as the union of two "hexagonal" bodies rotated 30 deg
apart; each hexagonal body is the intersection of three extruded profile slabs
(|u| <= apothem(z)), so every flank is a clean extruded surface.  Every ridge carries
a column of angled blind sockets (spine holes) and the top ring of sockets sits on
the dome.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
disc_r = 30.0          # base plate radius
disc_t = 2.4           # base plate thickness
n_ribs = 12            # ridges (two interleaved hexagons -> 12 ridges, valleys at 0.897 R)
slab_len = 80.0        # extrusion length of each profile slab (> body diameter)

# Ridge (peak) radius profile of the body, (r_peak, z):
#  - lower barrel: a gently flaring curve from the plate up to the widest section
#  - dome: a super-ellipse from the widest section up to the apex
barrel_pts = [
    (21.2, 0.0),
    (21.3, disc_t),
    (22.35, 23.5),
    (24.2, 47.6),
    (25.65, 62.0),
    (26.4, 74.0),
    (26.6, 83.0),
]
dome_z0 = 90.0         # height of the widest section where the dome starts
dome_rx = 26.6         # ridge radius at the widest section
dome_h = 24.7          # dome height above dome_z0 (apex at dome_z0 + dome_h)
dome_n = 2.3           # super-ellipse exponent (2 = ellipse, larger = flatter top)

# spine sockets along every ridge
spine_z = [43.5, 52.6, 63.0, 75.3, 89.8, 104.3, 112.4]   # socket heights on each ridge
hole_r = 1.3           # socket radius
hole_depth = 12.0      # socket depth below the ridge point
hole_tilt = [40.0] * 6 + [70.0]   # axis tilt below horizontal per row; top ring ~ dome normal

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- ridge profile ----------------
def _dome_pts():
    pts = []
    for zz in (0.0, 5.0, 10.0, 14.0, 17.5, 20.5, 22.6, 23.8, 24.4):
        t = zz / dome_h
        r = dome_rx * (1.0 - t ** dome_n) ** (1.0 / dome_n)
        pts.append((r, dome_z0 + zz))
    pts.append((0.0, dome_z0 + dome_h))
    return pts


ridge_profile = barrel_pts + _dome_pts()
z_apex = ridge_profile[-1][1]

cos30 = math.cos(math.radians(30))
apo = [(r * cos30, z) for r, z in ridge_profile]   # apothem profile of one hexagon


def slab_solid():
    """Symmetric profile |x| <= apothem(z) in the XZ plane, extruded along Y."""
    right = [cq.Vector(a, 0, z) for a, z in apo]
    t0 = (right[1] - right[0]).normalized()
    right_edge = cq.Edge.makeSpline(right, tangents=[t0, cq.Vector(-1, 0, 0)])
    left_edge = right_edge.mirror("YZ")
    bottom = cq.Edge.makeLine(
        cq.Vector(-apo[0][0], 0, apo[0][1]), cq.Vector(apo[0][0], 0, apo[0][1])
    )
    wire = cq.Wire.assembleEdges([bottom, right_edge, left_edge])
    face = cq.Face.makeFromWires(wire)
    sol = cq.Solid.extrudeLinear(face, cq.Vector(0, slab_len, 0))
    return sol.translate(cq.Vector(0, -slab_len / 2, 0)), right_edge


raw_slab, ridge_edge = slab_solid()


def rot(shape, ang):
    return shape.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), ang)


def star_body(trim):
    """Union of two hexagonal bodies; a hair is trimmed off the apex so the six
    slabs do not all meet in one tangent point."""
    box = cq.Solid.makeBox(4 * slab_len, 4 * slab_len, z_apex - trim + 1.0).translate(
        cq.Vector(-2 * slab_len, -2 * slab_len, -1.0)
    )
    s = raw_slab.intersect(box)
    hex_a = rot(s, 30).intersect(rot(s, 90)).intersect(rot(s, 150))   # peaks at 0, 60, ...
    hex_b = rot(s, 0).intersect(rot(s, 60)).intersect(rot(s, 120))    # peaks at 30, 90, ...
    return hex_a.fuse(hex_b).clean()


body = None
for trim in (0.001, 0.005, 0.02, 0.05):
    try:
        cand = star_body(trim)
        if cand.isValid() and len(cand.Solids()) == 1 and cand.Volume() > 1000.0:
            body = cand
            break
    except Exception:
        pass

# ---------------- base plate ----------------
disc = cq.Solid.makeCylinder(disc_r, disc_t, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1))
part = body.fuse(disc).clean()


# ---------------- spine sockets (angled blind holes on every ridge) ----------------
def apothem_at(z):
    """bisection on the ridge spline for the apothem at height z"""
    lo, hi = 0.0, 1.0
    for _ in range(60):
        mid = 0.5 * (lo + hi)
        if ridge_edge.positionAt(mid).z < z:
            lo = mid
        else:
            hi = mid
    return ridge_edge.positionAt(0.5 * (lo + hi)).x


holes = []
for zs, tilt in zip(spine_z, hole_tilt):
    rp = apothem_at(zs) / cos30          # ridge radius at this height
    ct, st = math.cos(math.radians(tilt)), math.sin(math.radians(tilt))
    for k in range(n_ribs):
        th = math.radians(360.0 / n_ribs * k)
        # axis runs into the body and downwards (a spine stuck in points up and out)
        d = cq.Vector(-ct * math.cos(th), -ct * math.sin(th), -st)
        c = cq.Vector(rp * math.cos(th), rp * math.sin(th), zs)
        start = c - d * 3.0
        holes.append(cq.Solid.makeCylinder(hole_r, 3.0 + hole_depth, start, d))

part = part.cut(cq.Compound.makeCompound(holes)).clean()

result = cq.Workplane("XY").add(part)
